import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # frame size along X
D = 100.0          # frame size along Y
T = 11.7           # overall height
T_DECK = 2.6       # thickness of the top deck (underside pocket ceiling)
WALL = 3.0         # side wall thickness (left / right)
WALL_F = 2.4       # front wall thickness
WALL_B = 3.6       # back wall thickness

# window layout (outline of the top recess), measured from the frame edges
BORDER_L = 7.3     # left border (-X side)
BORDER_R = 9.3     # right border (+X side)
BORDER_F = 12.1    # front border (-Y side)
BORDER_B = 14.1    # back border (+Y side)
BAR = 7.75         # middle bar between the two windows

RECESS_D = (2.85, 2.4)   # depth of the rounded top recess (left, right window)
RECESS_R = 1.3     # corner radius of the recess
LEDGE = 0.2        # small ledge between recess and the lower window
LIP_W = 1.8        # width of the stiffening lip around each window (underside)
LIP_H = (1.75, 1.5)      # how far each lip hangs below its recess floor

RIB_LIFT = 1.2     # bottom of the middle rib sits this far above the rim
POCKET_FIL = 1.5   # fillet where the middle rib meets the front/back walls
CORNER_FIL = 0.0   # fillet on the outer inside corners of the pocket

BOSS_R = 3.55      # screw boss radius
BOSS_OFF = 2.8     # boss centre distance outside the frame edge
BOSS_X = 0.4       # boss centre position along X
BOSS_HOLE = 3.6    # boss hole diameter
HOLE_DX = (-0.3, -0.7)   # hole offset from boss centre along X (front, back)
BOSS_FIL = 1.0     # fillet between boss and frame side

CORNER_HOLE = 3.5  # small hole near the back-right corner
CH_X = 8.3         # from right edge
CH_Y = 8.85        # from back edge

RIB_HOLE = 2.5     # blind hole in the underside of the middle rib
RIB_HOLE_DEPTH = 5.0

ROT_Z = 0.6        # the part sits rotated slightly about Z

# ---------------- derived layout ----------------
x0 = -W / 2 + BORDER_L
x3 = W / 2 - BORDER_R
win_w = (x3 - x0 - BAR) / 2.0
x1 = x0 + win_w
x2 = x1 + BAR
y0 = -D / 2 + BORDER_F
y1 = D / 2 - BORDER_B
win_l = y1 - y0
yc = (y0 + y1) / 2
xc1 = (x0 + x1) / 2
xc2 = (x2 + x3) / 2
bar_c = (x1 + x2) / 2
rib_w = BAR + 2 * LEDGE          # rib is flush with the lower window walls

z_ceil = T - T_DECK              # underside pocket ceiling
z_floor = [T - d for d in RECESS_D]                  # recess floors
z_lip = [zf - h for zf, h in zip(z_floor, LIP_H)]    # lip bottoms

# ---------------- main block ----------------
body = cq.Workplane("XY").box(W, D, T, centered=(True, True, False))

# screw bosses on the front and back faces, filleted into the sides
for sy in (-1, 1):
    boss = (
        cq.Workplane("XY")
        .center(BOSS_X, sy * (D / 2 + BOSS_OFF))
        .circle(BOSS_R)
        .extrude(T)
    )
    body = body.union(boss)
    body = body.edges(
        cq.selectors.BoxSelector(
            (BOSS_X - BOSS_R - 0.5, sy * D / 2 - 0.5, -1),
            (BOSS_X + BOSS_R + 0.5, sy * D / 2 + 0.5, T + 1),
        )
    ).fillet(BOSS_FIL)

# ---------------- underside: two pockets separated by the middle rib ----------------
pin_x = W / 2 - WALL
pin_y = D - WALL_F - WALL_B
pyc = (WALL_F - WALL_B) / 2.0     # pocket centre in Y
left_w = (bar_c - rib_w / 2) - (-pin_x)
right_w = pin_x - (bar_c + rib_w / 2)
pocket_l = (
    cq.Workplane("XY")
    .center(-pin_x + left_w / 2, pyc)
    .rect(left_w, pin_y)
    .extrude(z_ceil)
    .edges("|Z").edges(">X")
    .fillet(POCKET_FIL)
)
if CORNER_FIL > 0:
    pocket_l = pocket_l.edges("|Z").edges("<X").fillet(CORNER_FIL)
pocket_r = (
    cq.Workplane("XY")
    .center(pin_x - right_w / 2, pyc)
    .rect(right_w, pin_y)
    .extrude(z_ceil)
    .edges("|Z").edges("<X")
    .fillet(POCKET_FIL)
)
if CORNER_FIL > 0:
    pocket_r = pocket_r.edges("|Z").edges(">X").fillet(CORNER_FIL)
body = body.cut(pocket_l).cut(pocket_r)

# the rib stops a little short of the rim bottom
rib_relief = (
    cq.Workplane("XY")
    .workplane(offset=-1)
    .center(bar_c, pyc)
    .rect(rib_w + 2 * POCKET_FIL + 1, pin_y)
    .extrude(RIB_LIFT + 1)
)
body = body.cut(rib_relief)

# stiffening lips hanging under the deck around each window
for xc, zl in zip((xc1, xc2), z_lip):
    lip = (
        cq.Workplane("XY")
        .workplane(offset=zl)
        .center(xc, yc)
        .rect(win_w + 2 * LIP_W, win_l + 2 * LIP_W)
        .extrude(z_ceil - zl + 0.01)
    )
    body = body.union(lip)

# ---------------- windows ----------------
for xc, zf in zip((xc1, xc2), z_floor):
    # rounded recess from the top
    rec = (
        cq.Workplane("XY")
        .workplane(offset=zf)
        .center(xc, yc)
        .sketch()
        .rect(win_w, win_l)
        .vertices()
        .fillet(RECESS_R)
        .finalize()
        .extrude(T - zf + 1)
    )
    body = body.cut(rec)
    # sharp-cornered lower window through the lip
    win = (
        cq.Workplane("XY")
        .workplane(offset=-1)
        .center(xc, yc)
        .rect(win_w - 2 * LEDGE, win_l - 2 * LEDGE)
        .extrude(zf + 1)
    )
    body = body.cut(win)

# ---------------- holes ----------------
for sy, dx in zip((-1, 1), HOLE_DX):
    h = (
        cq.Workplane("XY")
        .workplane(offset=-1)
        .center(BOSS_X + dx, sy * (D / 2 + BOSS_OFF))
        .circle(BOSS_HOLE / 2)
        .extrude(T + 2)
    )
    body = body.cut(h)

ch = (
    cq.Workplane("XY")
    .workplane(offset=-1)
    .center(W / 2 - CH_X, D / 2 - CH_Y)
    .circle(CORNER_HOLE / 2)
    .extrude(T + 2)
)
body = body.cut(ch)

rh = (
    cq.Workplane("XY")
    .workplane(offset=-1)
    .center(bar_c, 0)
    .circle(RIB_HOLE / 2)
    .extrude(RIB_LIFT + RIB_HOLE_DEPTH + 1)
)
body = body.cut(rh)

result = body.rotate((0, 0, 0), (0, 0, 1), ROT_Z)

VIEW = {"azimuth": 45, "elevation": 26}
